"""Free-form teardrop bowl on a round foot disc.

The bowl is a smooth closed loft through horizontal cross-sections (an
egg/teardrop plan that narrows and rounds off toward the bottom), hollowed by
a second loft through inward offsets of the same sections, leaving a flat rim
band on top.  It sits on a plain cylindrical disc, offset toward the round
(+Y) end of the rim.  The pointed end of the teardrop faces -Y.
"""
import math
import cadquery as cq
from cadquery.func import loft as thru_sections

# ---------------- driving dimensions (mm) ----------------
RIM_L = 100.0          # rim length along Y (teardrop, pointed end toward -Y)
RIM_W = 84.6           # rim width along X
RIM_YW = 12.0          # Y of the widest point of the rim (from rim centre)
TOTAL_H = 67.0         # overall height (disc bottom to rim top)
WALL = 3.4             # bowl wall thickness (normal to the surface)
RIM_BAND = 3.65        # width of the flat rim band seen from above
FLOOR_T = 3.8          # floor thickness under the flat inside floor
FLOOR_Y = 12.0         # Y position of the flat inside floor
FLOOR_R = 4.0          # radius of the flat inside floor
DISC_D = 50.0          # foot disc diameter
DISC_T = 8.4           # foot disc thickness
DISC_DY = 11.6         # disc centre offset toward +Y from the rim centre
FOOT_Y = 9.8           # Y of the lowest point of the bowl (sits on the disc)
FOOT_R = 3.5           # radius of the bowl's contact patch on the disc
EMBED = 0.1            # how far the contact patch sinks into the disc (fusion)

# The cross-section table below is written for a reference bowl of
# 100 x 84.6 mm rim and 58.6 mm bowl height; it is scaled to the values above.
REF_L, REF_W, REF_H = 100.0, 84.6, 58.6
SX = RIM_W / REF_W
SY = RIM_L / REF_L
SZ = (TOTAL_H - DISC_T) / REF_H

# Teardrop "-Y half" of a section: half-width fraction f versus the fraction
# s of the distance from the widest point to the tip (rim measured from top).
TEAR_S = [0.0, 0.155, 0.281, 0.406, 0.553, 0.679, 0.784, 0.889, 0.963, 1.0]
TEAR_F = [1.0, 0.960, 0.896, 0.804, 0.681, 0.558, 0.437, 0.281, 0.128, 0.0]
TEAR_F_BLUNT = [1.0, 0.960, 0.896, 0.804, 0.681, 0.558, 0.437, 0.285, 0.175, 0.0]
TEAR_F_HOLLOW = [1.0, 0.945, 0.860, 0.745, 0.600, 0.475, 0.370, 0.250, 0.125, 0.0]

# sample stations used for every cross-section (same count -> clean loft)
LOW_S = [0.955, 0.86, 0.72, 0.55, 0.36, 0.17]     # -Y half
UP_T = [1.25, 0.95, 0.65, 0.33]                   # +Y half (angle param)

# Bowl cross-sections, bottom to rim (reference mm):
# (height above disc top, ymin, ymax, half-width, y of widest,
#  -Y roundness k, +Y superellipse n, -Y superellipse m, tip shape tb)
#   k = 0: teardrop -Y half, k = 1: superellipse -Y half
#   tb > 0: blunter tip (rim), tb < 0: hollow-flanked spout (mid height)
SECTIONS = [
    (0.6, 4.5, 15.1, 5.3, 9.8, 1.0, 2.0, 2.0, 0.0),
    (2.1, 1.8, 18.8, 8.4, 10.3, 1.0, 2.0, 2.1, 0.0),
    (4.1, -1.2, 23.1, 11.5, 11.0, 1.0, 2.0, 2.2, 0.0),
    (7.6, -4.0, 27.9, 16.4, 12.0, 0.9, 2.0, 2.2, 0.0),
    (13.6, -15.5, 33.0, 22.4, 12.0, 0.6, 2.2, 2.2, 0.0),
    (23.6, -30.9, 37.9, 28.4, 11.0, 0.3, 2.25, 2.0, -0.7),
    (36.6, -41.5, 42.7, 34.3, 10.5, 0.05, 1.95, 2.0, -1.0),
    (47.6, -45.9, 46.2, 38.0, 11.0, 0.03, 1.95, 2.0, -0.5),
    (REF_H, -REF_L / 2, REF_L / 2, REF_W / 2, RIM_YW / SY, 0.0, 1.9, 2.0, 1.0),
]
INNER_FROM = 7.6       # sections at/above this height also shape the cavity


def tear_f(s, tb=0.0):
    """teardrop half-width fraction; tb > 0 blends toward the blunter rim
    tip, tb < 0 toward the hollow-flanked spout of the mid sections"""
    alt = TEAR_F_BLUNT if tb >= 0 else TEAR_F_HOLLOW
    w = abs(tb)
    tab = [(1 - w) * f0 + w * f1 for f0, f1 in zip(TEAR_F, alt)]
    for i in range(len(TEAR_S) - 1):
        if TEAR_S[i] <= s <= TEAR_S[i + 1]:
            t = (s - TEAR_S[i]) / (TEAR_S[i + 1] - TEAR_S[i])
            return tab[i] * (1 - t) + tab[i + 1] * t
    return 0.0


def section_pts(ymin, ymax, a, yw, k, n=2.0, m=2.0, tb=0.0):
    """Closed, X-symmetric cross-section (list of XY points) starting at the
    -Y tip: +Y half a superellipse, -Y half a teardrop/superellipse blend."""
    right = []
    for s in LOW_S:
        f = (1 - k) * tear_f(s, tb) + k * max(0.0, 1 - s ** m) ** (1.0 / m)
        right.append((a * f, yw - (yw - ymin) * s))
    right.append((a, yw))
    e = 2.0 / n
    for t in UP_T:
        right.append((a * math.sin(t) ** e, yw + (ymax - yw) * math.cos(t) ** e))
    pts = [(0.0, ymin)] + right + [(0.0, ymax)]
    pts += [(-x, y) for (x, y) in reversed(right)]
    return pts


def make_wire(pts, z):
    """Closed periodic spline through the points, at height z."""
    vs = [cq.Vector(x, y, z) for (x, y) in pts]
    # identical (uniform) parameterisation for every section so that the
    # loft connects corresponding points without twisting
    e = cq.Edge.makeSpline(vs, periodic=True,
                           parameters=[float(i) for i in range(len(vs) + 1)])
    return cq.Wire.assembleEdges([e])


def loft(wires):
    """Smooth capped loft: cubic, C2, chord-length spacing between sections
    (keeps the skin from overshooting between unevenly spaced sections)."""
    return thru_sections(wires, cap=True, ruled=False, continuity="C2",
                         parametrization="chordal", degree=3, compat=False)


# ---------------- outer skin ----------------
outer_pts = []
# contact patch, sunk slightly into the disc so the two bodies fuse
outer_pts.append((section_pts(FOOT_Y - FOOT_R, FOOT_Y + FOOT_R, FOOT_R,
                              FOOT_Y, 1.0), DISC_T - EMBED, False))
for (h, ymn, ymx, a, yw, k, n, m, tb) in SECTIONS:
    pts = section_pts(ymn * SY, ymx * SY, a * SX, yw * SY, k, n, m, tb)
    outer_pts.append((pts, DISC_T + h * SZ, h >= INNER_FROM))
outer = loft([make_wire(p, z) for (p, z, _) in outer_pts])
skin = max(outer.Faces(), key=lambda f: f.Area())


def inner_section(pts, z, fixed=None, cap=2.6):
    """Offset a section inward so the wall has normal thickness WALL:
    horizontal offset = WALL / |horizontal part of the surface normal|
    (or a fixed horizontal offset, used for the flat rim band)."""
    cx = sum(p[0] for p in pts) / len(pts)
    cy = sum(p[1] for p in pts) / len(pts)
    res = []
    for (x, y) in pts:
        nrm = skin.normalAt(cq.Vector(x, y, z))
        nx, ny = nrm.x, nrm.y
        if nx * (x - cx) + ny * (y - cy) < 0:      # make it point outward
            nx, ny = -nx, -ny
        h = math.hypot(nx, ny)
        d = fixed if fixed is not None else WALL / max(h, 1.0 / cap)
        res.append((x - d * nx / h, y - d * ny / h))
    return res


# ---------------- cavity ----------------
inner_wires = [make_wire(section_pts(FLOOR_Y - FLOOR_R, FLOOR_Y + FLOOR_R,
                                     FLOOR_R, FLOOR_Y, 1.0), DISC_T + FLOOR_T)]
for (p, z, use) in outer_pts:
    if use:
        band = RIM_BAND if z >= TOTAL_H - 1e-6 else None
        inner_wires.append(make_wire(inner_section(p, z, band), z))
inner = loft(inner_wires)
# carry the cavity straight up through the rim plane for a clean cut
rim_face = cq.Face.makeFromWires(inner_wires[-1])
plug = cq.Solid.extrudeLinear(rim_face, cq.Vector(0, 0, 5.0))
cavity = inner.fuse(plug).clean()

bowl = outer.cut(cavity)

# ---------------- foot disc ----------------
disc = (cq.Workplane("XY").circle(DISC_D / 2).extrude(DISC_T)
        .rotate((0, 0, 0), (0, 0, 1), 225)         # park the seam at -X-Y
        .translate((0, DISC_DY, 0)))

result = disc.union(cq.Workplane("XY").add(bowl))
